import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R = 50.0            # outer radius of main pipe and of the branch
H = 148.4           # overall height of main pipe (incl. lid)
ZB = 75.3           # height of branch axis above the bottom
L_BR = 59.4         # branch end distance from main axis (+Y)
T_BR = 0.5          # branch sheet wall thickness (open branch end)

LID_H = 6.9         # height of top lid skirt
LID_GAP = 0.15      # lid skirt radial overhang
LID_T = 1.0         # lid skirt sheet thickness

BOT_BAND_H = 5.3    # bottom cover band height (below the bead groove)
BOT_BAND_IN = 0.4   # radial inset of bottom cover band
GROOVE_TOP = 8.5    # top of the trapezoidal bead groove
GROOVE_BEV = 0.5    # height of the groove bevels
GROOVE_D = 0.65     # groove depth

N_SCREW = 6
SCREW_BC = 43.5     # bolt circle radius of bottom cover screws
SCREW_D = 7.0       # screw head diameter
SCREW_HT = 0.6      # screw head height (below bottom face)
SCREW_DOME = 0.4    # domed part of the head
CROSS_L = 3.0       # cross recess length
CROSS_W = 0.7       # cross recess slot width
CROSS_DEPTH = 0.5   # cross recess depth
SCREW_A0 = 30.0     # angle of first screw (deg from +X)


def plane(origin, xdir, normal):
    return cq.Workplane(cq.Plane(origin=origin, xDir=xdir, normal=normal))


# ---------------- main pipe (closed body), revolved profile ----------------
# profile in the local (radius, height) plane; bead groove and bottom band included
profile = [
    (0.0, 0.0),
    (R - BOT_BAND_IN, 0.0),
    (R - BOT_BAND_IN, BOT_BAND_H),
    (R - GROOVE_D, BOT_BAND_H + GROOVE_BEV),
    (R - GROOVE_D, GROOVE_TOP - GROOVE_BEV),
    (R, GROOVE_TOP),
    (R, H),
    (0.0, H),
]
# sketch on the plane spanned by +Y (radius) and +Z so the seam sits at +Y, under the branch
main = (
    plane((0, 0, 0), (0, 1, 0), (1, 0, 0))
    .polyline(profile)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)

# ---------------- branch: thin open tube along +Y ----------------
sq = math.sqrt(0.5)
branch = (
    plane((0, 0, ZB), (-sq, 0, -sq), (0, 1, 0))
    .circle(R)
    .circle(R - T_BR)
    .extrude(L_BR)
)
body = main.union(branch)

# ---------------- top lid skirt ----------------
lid = (
    plane((0, 0, H - LID_H), (0, 1, 0), (0, 0, 1))
    .circle(R + LID_GAP)
    .circle(R + LID_GAP - LID_T)
    .extrude(LID_H)
)
body = body.union(lid)

# ---------------- bottom cover screws (pan heads, cross recess) ----------------
sph_r = (SCREW_DOME ** 2 + (SCREW_D / 2) ** 2) / (2 * SCREW_DOME)
for i in range(N_SCREW):
    a = math.radians(SCREW_A0 + i * 360.0 / N_SCREW)
    x, y = SCREW_BC * math.cos(a), SCREW_BC * math.sin(a)
    zc = -(SCREW_HT - SCREW_DOME)          # lower end of the cylindrical rim of the head
    rim = (
        cq.Workplane("XY", origin=(x, y, zc))
        .circle(SCREW_D / 2)
        .extrude(SCREW_HT - SCREW_DOME + 0.05)
    )
    dome = (
        cq.Workplane("XY")
        .sphere(sph_r)
        .translate((x, y, zc + sph_r - SCREW_DOME))
        .intersect(
            cq.Workplane("XY", origin=(x, y, -SCREW_HT - 0.01))
            .circle(SCREW_D / 2)
            .extrude(SCREW_DOME + 0.02)
        )
    )
    head = rim.union(dome)
    cross = (
        cq.Workplane("XY", origin=(x, y, -SCREW_HT - 0.5))
        .transformed(rotate=(0, 0, math.degrees(a) + 45.0))
        .rect(CROSS_L, CROSS_W)
        .extrude(CROSS_DEPTH + 0.5)
        .union(
            cq.Workplane("XY", origin=(x, y, -SCREW_HT - 0.5))
            .transformed(rotate=(0, 0, math.degrees(a) + 45.0))
            .rect(CROSS_W, CROSS_L)
            .extrude(CROSS_DEPTH + 0.5)
        )
    )
    body = body.union(head.cut(cross))

result = body

VIEW = {"azimuth": 45, "elevation": 26}
